import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
MODULE = 2.0            # gear module
TEETH = 24              # number of teeth
PRESSURE_ANGLE = 20.0   # deg
ADDENDUM = 1.0 * MODULE
ROOT_DIA = 44.4         # root circle diameter
FACE_WIDTH = 9.45       # gear thickness (Z)

BORE_DIA = 18.9         # through bore
CBORE_DIA = 23.2        # counterbore from the top face
CBORE_DEPTH = 8.1       # counterbore depth

BOSS_DIA = 9.1          # eccentric boss on the top face
BOSS_HEIGHT = 8.05      # above the top face
BOSS_OFFSET = 17.45     # distance of boss axis from gear axis (+X)
BOSS_HOLE_DIA = 3.7     # blind hole in the boss
BOSS_HOLE_DEPTH = BOSS_HEIGHT  # down to the gear face

FLANK_PTS = 7           # spline points per involute flank
SEAM_ANGLE = 45.0       # where cylinder seams sit (least visible)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
r_p = MODULE * TEETH / 2.0
r_a = r_p + ADDENDUM
r_f = ROOT_DIA / 2.0
alpha = math.radians(PRESSURE_ANGLE)
r_b = r_p * math.cos(alpha)


def inv(a):
    return math.tan(a) - a


# half tooth angle measured at the base circle
psi_b = math.pi / (2 * TEETH) + inv(alpha)


def half_angle(r):
    """half angular thickness of the tooth at radius r (r >= r_b)."""
    a = math.acos(min(1.0, r_b / r))
    return psi_b - inv(a)


def pol(r, ang):
    return (r * math.cos(ang), r * math.sin(ang))


def flank_point(c, r, side):
    """point on the flank of the tooth centred at angle c; side=-1 lower, +1 upper.
    Below the base circle the flank continues radially down to the root."""
    h = half_angle(max(r, r_b))
    return pol(r, c + side * h)


def flank_dir(c, r, side, sign):
    """unit tangent of the flank at radius r (sign=+1 outward, -1 inward)."""
    if r <= r_b + 1e-9:
        d = (math.cos(c + side * half_angle(r_b)), math.sin(c + side * half_angle(r_b)))
    else:
        dr = 1e-4
        p0 = flank_point(c, r - dr, side)
        p1 = flank_point(c, r, side)
        d = (p1[0] - p0[0], p1[1] - p0[1])
    n = math.hypot(*d)
    return (sign * d[0] / n, sign * d[1] / n)


def gear_profile():
    pitch = 2 * math.pi / TEETH
    r_start = max(r_b, r_f)
    # flank stations: root, (base circle), then involute up to the tip
    radii = [r_start + (r_a - r_start) * (i / (FLANK_PTS - 1)) ** 1.3
             for i in range(FLANK_PTS)]
    if r_f < r_b:
        radii = [r_f] + radii
    wp = cq.Workplane("XY")
    for k in range(TEETH):
        c = k * pitch
        lower = [flank_point(c, r, -1) for r in radii]
        upper = [flank_point(c, r, +1) for r in reversed(radii)]
        if k == 0:
            wp = wp.moveTo(*lower[0])
        else:
            # root arc from the previous tooth to this one
            wp = wp.threePointArc(pol(r_f, c - pitch / 2.0), lower[0])
        # one smooth face per flank (radial foot blends tangentially into the involute)
        wp = wp.spline(lower[1:], includeCurrent=True,
                       tangents=[flank_dir(c, radii[0], -1, 1),
                                 flank_dir(c, r_a, -1, 1)])
        wp = wp.threePointArc(pol(r_a, c), upper[0])
        wp = wp.spline(upper[1:], includeCurrent=True,
                       tangents=[flank_dir(c, r_a, +1, -1),
                                 flank_dir(c, radii[0], +1, -1)])
    # last root arc back to the start point
    c_last = (TEETH - 1) * pitch
    start = flank_point(0.0, radii[0], -1)
    wp = wp.threePointArc(pol(r_f, c_last + pitch / 2.0), start)
    return wp.close()


def cyl(x, y, z0, dia, h):
    """vertical cylinder; its seam line is placed at SEAM_ANGLE."""
    a = math.radians(SEAM_ANGLE)
    pl = cq.Plane(origin=(x, y, z0), xDir=(math.cos(a), math.sin(a), 0),
                  normal=(0, 0, 1))
    return cq.Workplane(pl).circle(dia / 2.0).extrude(h)


gear = gear_profile().extrude(FACE_WIDTH)

# through bore + counterbore from the top face
gear = gear.cut(cyl(0, 0, -1.0, BORE_DIA, FACE_WIDTH + 2.0))
gear = gear.cut(cyl(0, 0, FACE_WIDTH - CBORE_DEPTH, CBORE_DIA, CBORE_DEPTH + 1.0))

# eccentric boss with blind hole
gear = gear.union(cyl(BOSS_OFFSET, 0, FACE_WIDTH, BOSS_DIA, BOSS_HEIGHT))
gear = gear.cut(cyl(BOSS_OFFSET, 0, FACE_WIDTH + BOSS_HEIGHT - BOSS_HOLE_DEPTH,
                    BOSS_HOLE_DIA, BOSS_HOLE_DEPTH + 1.0))

result = gear
